import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
D = 60.0            # outer diameter of the round case
L = 23.0            # axial length (along Y); front face closed at -Y, open at +Y
WALL = 2.7          # side wall thickness
FLOOR = 2.0         # thickness of the closed front face

KNOB_W = 11.6       # knob / window width along Y
KNOB_Z0 = -3.0      # knob bottom (Z)
KNOB_Z1 = 3.0       # knob top (Z)
KNOB_OUT = 2.7      # knob protrusion beyond the case outer radius
KNOB_FIL = 0.9      # fillet on the lower outline of the lever (knob lower edge)

HOLE_R = 3.67       # round window above the +X knob
HOLE_Y = -2.73
HOLE_Z = 3.0

POST_X0 = 1.3       # square posts standing on the floor
POST_X1 = 7.7
POST_ZA = 6.67      # inner face (|Z|) of the posts
POST_ZB = 12.75     # outer face (|Z|) of the posts
POST_TOP = -0.85    # Y of the post tops

BAR_NEAR = (5.6, 5.0, 4.0, 3.6)  # lever near (+Y) face at X = +23.9, +12, -13, -23.9
BAR_FAR = (-6.3, -5.0)           # lever far (-Y) face at X = +23.9 and from X = +7.4 to -X end
BAR_FIL = 1.2       # fillet on the upper outline of the lever (knob top edge)
PLAN_FIL = 3.0      # plan-view blend between heads and bar
RACK_X0, RACK_X1 = -11.5, 13.0   # recessed (toothed) stretch of the lever underside
RACK_TOP = 0.6      # Z of the recess roof
TOOTH_Z0 = -1.6     # Z of the tooth tips
TOOTH_W = 0.9       # tooth width along X
TOOTH_D = 2.4       # tooth depth along Y
TOOTH_SET = -1.0    # set-back of the teeth from the near face (negative: standing proud)
POCKET_X0 = -17.0   # stepped pocket in the lever top near the -X end
POCKET_X1, POCKET_D1 = -8.7, 0.8
POCKET_X2, POCKET_D2 = -10.0, 1.6
POCKET_Y0, POCKET_Y1 = -2.6, 2.4
TEETH_X_START = 12.0             # +X face of the first tooth of each group
TEETH_GAPS_A = (1.25, 1.45, 2.3, 2.8, 2.7)
TEETH_X_START2 = -0.1
TEETH_GAPS_B = (1.25, 1.45, 2.3, 2.8, 2.7)

R = D / 2.0
RI = R - WALL
Y0, Y1 = -L / 2.0, L / 2.0
YF = Y0 + FLOOR

# workplane normal to -Y whose x-direction puts cylinder seams on the hidden lower-left side
seam_dir = (-math.sqrt(0.5), 0.0, -math.sqrt(0.5))


def yplane(y):
    return cq.Workplane(cq.Plane(origin=(0, y, 0), xDir=seam_dir, normal=(0, -1, 0)))


# ---------------- case (cup) ----------------
case = yplane(Y1).circle(R).extrude(L)               # from Y1 towards -Y
cavity = yplane(Y1 + 1.0).circle(RI).extrude(L - FLOOR + 1.0)
case = case.cut(cavity)

# round window above the +X knob
hole = (
    cq.Workplane("YZ", origin=(RI - 1.0, 0, 0))
    .center(HOLE_Y, HOLE_Z)
    .circle(HOLE_R)
    .extrude(WALL + 3.0)
)
case = case.cut(hole)

# ---------------- lever ----------------
# Each end of the lever is a round head (disc in plan) whose outer part pokes
# through the side wall as the knob; a tapered bar joins the two heads.
kh = KNOB_Z1 - KNOB_Z0
xa = R + KNOB_OUT                       # apex of knob arc
yc = KNOB_W / 2.0
xe = math.sqrt(R * R - yc * yc)         # where the knob arc meets the outer wall
sag = xa - xe
rk = (yc * yc + sag * sag) / (2 * sag)  # head radius in plan
xc = xa - rk                            # head centre (|X|)


def head(sign):
    return (
        cq.Workplane("XY", origin=(0, 0, KNOB_Z0))
        .center(sign * xc, 0)
        .circle(rk)
        .extrude(kh)
    )


xb = xc - 2.0                           # bar ends hidden inside the heads
bar = (
    cq.Workplane("XY", origin=(0, 0, KNOB_Z0))
    .moveTo(xb, BAR_NEAR[0])
    .threePointArc((12.0, BAR_NEAR[1]), (-13.0, BAR_NEAR[2]))
    .lineTo(-xb, BAR_NEAR[3])
    .lineTo(-xb, BAR_FAR[1])
    .lineTo(7.4, BAR_FAR[1])
    .lineTo(xb, BAR_FAR[0])
    .close()
    .extrude(kh)
)
bar = bar.union(head(1)).union(head(-1))
zm = (KNOB_Z0 + KNOB_Z1) / 2.0
# blend the heads into the bar (vertical edges only)
bar = bar.edges(cq.selectors.BoxSelector((-40, -20, zm - 0.5), (40, 20, zm + 0.5))).fillet(PLAN_FIL)
bar = bar.faces(">Z").edges().fillet(BAR_FIL)
# round the lower outline (gives the knobs their rounded lower edge)
bar = bar.faces("<Z").edges().fillet(KNOB_FIL)

# stepped pocket in the top near the -X end
for x0, dz in ((POCKET_X1, POCKET_D1), (POCKET_X2, POCKET_D2)):
    pk = (
        cq.Workplane("XY")
        .box(x0 - POCKET_X0, POCKET_Y1 - POCKET_Y0, dz + 1.0, centered=False)
        .translate((POCKET_X0, POCKET_Y0, KNOB_Z1 - dz))
    )
    bar = bar.cut(pk)

# underside recess over the rack stretch
recess = (
    cq.Workplane("XY")
    .box(RACK_X1 - RACK_X0, 20.0, RACK_TOP - KNOB_Z0 + 1.0, centered=False)
    .translate((RACK_X0, -10.0, KNOB_Z0 - 1.0))
)
bar = bar.cut(recess)

# rack teeth hanging in the recess, standing slightly proud of the near face
def near_y(x):
    return BAR_NEAR[2] + (x + 13.0) * (BAR_NEAR[1] - BAR_NEAR[2]) / 25.0


teeth_x = []
for g0, gaps in ((TEETH_X_START, TEETH_GAPS_A), (TEETH_X_START2, TEETH_GAPS_B)):
    xx = g0
    teeth_x.append(xx)
    for gp in gaps:
        xx -= gp
        teeth_x.append(xx)
for xt in teeth_x:
    yn = near_y(xt)
    t = (
        cq.Workplane("XY")
        .box(TOOTH_W, TOOTH_D, RACK_TOP - TOOTH_Z0 + 0.2, centered=False)
        .translate((xt - TOOTH_W, yn - TOOTH_SET - TOOTH_D, TOOTH_Z0))
    )
    bar = bar.union(t)

lever = bar

# ---------------- square posts on the floor ----------------
ph = POST_TOP - YF + 0.01
for zlo, zhi in ((POST_ZA, POST_ZB), (-POST_ZB, -POST_ZA)):
    p = (
        cq.Workplane("XY")
        .box(POST_X1 - POST_X0, ph, zhi - zlo, centered=False)
        .translate((POST_X0, YF - 0.01, zlo))
    )
    case = case.union(p)

result = case.union(lever)
